import math
import cadquery as cq

# ============ driving dimensions (mm) ============
L = 90.0        # length along Y (front -Y ... back +Y)
W = 26.3        # width along X
H = 35.6        # height along Z (top of front wall / rails)
T = 2.2         # side wall thickness
TB = 2.0        # floor thickness
R = 4.0         # vertical (plan) corner radius, outside
RB = 3.5        # fillet on the bottom outside edges
RF = 1.2        # inside floor-to-wall fillet

# sliding-lid groove along both long walls and the front wall
LIP_H = 2.0         # height of the lip above the groove
GROOVE_H = 1.5      # groove height
LIP_RECESS = 0.4    # lip inner face set back from wall inner face
GROOVE_DEPTH = 1.0  # groove back set back from wall inner face
NOTCH_D = 3.8       # back end is lower by this much (lid entry)

# front cable slot (stadium)
FS_W = 10.0
FS_H = 4.0
FS_Z = 10.7

# floor features
BOSS_X, BOSS_Y = 0.4, 4.6
BOSS_D = 7.5
BOSS_H = 4.0
BOSS_HOLE = 1.5     # small through hole in the boss
BOSS_CSK = 2.4      # countersink diameter at the top of the boss
BOSS_R = 0.45       # chamfer on the boss top edge
HOLE_X, HOLE_Y = 6.4, -4.35
HOLE_D = 4.0
SLOT_L = 12.3
SLOT_W = 1.8
SLOT_YS = (-24.0, -28.0, -32.0)
PAD = 4.9
PAD_H = 4.0

# raised marking on the underside
EMB = 0.35          # emboss height
RIM = 0.25          # thin raised rim around each vent slot
TXT = "Spindel"
TXT_SIZE = 8.2
TXT_GAP = 0.55      # gap between letters
TXT_BASE_X = 3.65   # baseline position (letters grow towards -X)
TXT_START_Y = 2.9   # first letter starts here, text runs towards -Y


def rrect(w, l, r, z0, h):
    """rounded-rectangle prism centred on the Z axis from z0 up by h"""
    return (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .sketch()
        .rect(w, l)
        .vertices()
        .fillet(r)
        .finalize()
        .extrude(h)
    )


# ============ outer shell ============
body = rrect(W, L, R, 0, H)
body = body.faces("<Z").edges().fillet(RB)

# main cavity with a small fillet where the floor meets the walls
ri = R - T
cavity = rrect(W - 2 * T, L - 2 * T, ri, TB, H)
cavity = cavity.faces("<Z").edges().fillet(RF)
body = body.cut(cavity)

# lip recess (top band) and lid groove (below the lip)
o = LIP_RECESS
body = body.cut(rrect(W - 2 * T + 2 * o, L - 2 * T + 2 * o, ri + o, H - LIP_H, LIP_H + 1))
g = GROOVE_DEPTH
body = body.cut(
    rrect(W - 2 * T + 2 * g, L - 2 * T + 2 * g, ri + g, H - LIP_H - GROOVE_H, GROOVE_H)
)

# back end lowered so that the lid can slide in
notch = (
    cq.Workplane("XY")
    .box(W + 2, R + 1, NOTCH_D + 1, centered=(True, False, False))
    .translate((0, L / 2 - R, H - NOTCH_D))
)
body = body.cut(notch)

# ============ floor features (inside) ============
# corner pads
px = W / 2 - T - PAD / 2
py = L / 2 - T - PAD / 2
pads = (
    cq.Workplane("XY")
    .workplane(offset=TB - 0.5)
    .pushPoints([(sx * px, sy * py) for sx in (-1, 1) for sy in (-1, 1)])
    .rect(PAD, PAD)
    .extrude(PAD_H + 0.5)
)
body = body.union(pads)

# screw boss
boss = (
    cq.Workplane("XY")
    .workplane(offset=TB - 0.5)
    .center(BOSS_X, BOSS_Y)
    .circle(BOSS_D / 2)
    .extrude(BOSS_H + 0.5)
    .faces(">Z")
    .edges()
    .chamfer(BOSS_R)
)
body = body.union(boss)

# ============ raised marking on the underside ============
Z0 = 0.2                 # start slightly inside the floor so the union is clean
EH = EMB + Z0            # total height of the marking solids (grown downwards)


def down(wp):
    """extrude a 2D Workplane sketch from z=Z0 down to z=-EMB"""
    return wp.extrude(-EH)


def base():
    return cq.Workplane("XY").workplane(offset=Z0)


emboss = None


def add(shape):
    global emboss
    emboss = shape if emboss is None else emboss.union(shape)


# thin rims around the vent slots
add(down(base().pushPoints([(0, y) for y in SLOT_YS]).slot2D(SLOT_L + 2 * RIM, SLOT_W + 2 * RIM, 0)))

# molecule logo: three rings joined by bars
mol = [
    ((BOSS_X, BOSS_Y), 2.4, 1.5),     # ring around the screw-boss hole
    ((7.0, 10.2), 2.4, 1.5),
    ((-4.0, 13.8), 4.5, 3.1),
]
bar_w = 0.8
for i in range(3):
    for j in range(i + 1, 3):
        (x1, y1), _, _ = mol[i]
        (x2, y2), _, _ = mol[j]
        ln = math.hypot(x2 - x1, y2 - y1)
        ang = math.degrees(math.atan2(y2 - y1, x2 - x1))
        add(
            down(
                base()
                .center((x1 + x2) / 2, (y1 + y2) / 2)
                .transformed(rotate=(0, 0, ang))
                .rect(ln, bar_w)
            )
        )
for (cx, cy), ro, rin in mol:
    add(down(base().center(cx, cy).circle(ro)))
for (cx, cy), ro, rin in mol:
    emboss = emboss.cut(
        cq.Workplane("XY").workplane(offset=-2).center(cx, cy).circle(rin).extrude(4)
    )

# thermometer icon
TH_Y = 31.6          # axis of the thermometer (runs along X)
TH_BX = 4.9          # bulb centre X
TH_RO, TH_RI = 2.5, 1.75
add(down(base().center(-0.7, TH_Y).slot2D(10.0, 2.6, 0)))
add(down(base().center(TH_BX, TH_Y).circle(TH_RO)))
emboss = emboss.cut(
    cq.Workplane("XY").workplane(offset=-2).center(-0.7, TH_Y).slot2D(9.0, 1.6, 0).extrude(4)
)
emboss = emboss.cut(
    cq.Workplane("XY").workplane(offset=-2).center(TH_BX, TH_Y).circle(TH_RI).extrude(4)
)
add(down(base().center(-0.5, TH_Y).slot2D(7.8, 0.7, 0)))
add(down(base().center(TH_BX, TH_Y).circle(1.0)))
add(
    down(
        base()
        .pushPoints([(-4.0 + 1.2 * k, TH_Y + 3.2) for k in range(5)])
        .rect(0.4, 1.2)
    )
)

# drop icon
DR_C = (2.8, 23.5)
DR_R = 2.9
DR_TIP = (-3.4, 23.3)
d = DR_C[0] - DR_TIP[0]
a = math.acos(DR_R / d)           # tangent angle from the tip side
t1 = (DR_C[0] - DR_R * math.cos(a), DR_C[1] + DR_R * math.sin(a))
t2 = (DR_C[0] - DR_R * math.cos(a), DR_C[1] - DR_R * math.sin(a))
drop = (
    base()
    .moveTo(*DR_TIP)
    .lineTo(*t1)
    .threePointArc((DR_C[0] + DR_R, DR_C[1]), t2)
    .close()
)
drop_solid = down(drop)
drop_in = drop_solid.faces("<Z").wires().toPending().offset2D(-0.6).extrude(EH + 1, combine=False)
add(drop_solid.cut(drop_in.translate((0, 0, -0.5))))
add(down(base().center(-1.8, 26.4).transformed(rotate=(0, 0, 25)).ellipse(2.0, 0.8)))

# lettering, read correctly from below; runs from the logo towards the slots.
# letters are set one by one with tight spacing (narrow logo type)
try:
    ycur = TXT_START_Y
    for ch in TXT:
        glyph = (
            cq.Workplane("XY")
            .text(ch, TXT_SIZE, EH, combine=False, halign="left", valign="bottom")
            .val()
        )
        gb = glyph.BoundingBox()
        # glyph x -> world -Y, glyph y (up) -> world -X, extrusion -> world -Z
        glyph = glyph.moved(cq.Location(cq.Vector(-gb.xmin, 0, 0)))
        glyph = glyph.moved(cq.Location(cq.Vector(0, 0, 0), cq.Vector(1, -1, 0), 180))
        glyph = glyph.moved(cq.Location(cq.Vector(TXT_BASE_X, ycur, Z0)))
        add(cq.Workplane("XY").add(glyph).combine())
        ycur -= (gb.xmax - gb.xmin) + TXT_GAP
except Exception:
    pass

body = body.union(emboss)

# ============ holes & slots through the floor ============
body = body.cut(
    cq.Workplane("XY").workplane(offset=-2).center(BOSS_X, BOSS_Y).circle(BOSS_HOLE / 2).extrude(TB + BOSS_H + 4)
)
csk_h = (BOSS_CSK - BOSS_HOLE) / 2          # 90 degree countersink
csk = cq.Solid.makeCone(
    BOSS_HOLE / 2, BOSS_CSK / 2 + 0.5, csk_h + 0.5,
    cq.Vector(BOSS_X, BOSS_Y, TB + BOSS_H - csk_h), cq.Vector(0, 0, 1),
)
body = body.cut(cq.Workplane("XY").add(csk))
body = body.cut(
    cq.Workplane("XY").workplane(offset=-2).center(HOLE_X, HOLE_Y).circle(HOLE_D / 2).extrude(TB + 4)
)
slots = (
    cq.Workplane("XY")
    .workplane(offset=-2)
    .pushPoints([(0, y) for y in SLOT_YS])
    .slot2D(SLOT_L, SLOT_W, 0)
    .extrude(TB + 4)
)
body = body.cut(slots)

# ============ front cable slot ============
fslot = (
    cq.Workplane("XZ", origin=(0, -L / 2 - 1, 0))
    .center(0, FS_Z)
    .slot2D(FS_W, FS_H, 0)
    .extrude(-(T + 2))
)
body = body.cut(fslot)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
